import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R1 = 50.0          # knurled grip band outer radius
LK = 13.84         # grip band axial length (grid face -> shoulder)
CH = 4.0           # chamfer on grid-end outer edge (45 deg)
FK = 1.7           # fillet on shoulder outer edge
GW = 3.3           # width of semicircular relief groove in shoulder face
RT = 43.0          # thread crest radius
TD = 0.9           # thread groove depth
TW = 1.0           # thread crest / groove width
RN = 41.4          # neck radius in front of the rim bead
RM = 42.5          # rim bead radius
L = 21.8           # overall axial length
RI = 38.0          # bore radius
TG = 1.0           # grid plate thickness
FR = (RM - RI) / 2.0  # rim bead: full round of the rim end

# hex grid
RG = 37.0          # radius of perforated zone
HEX_PITCH = 11.0   # centre distance of neighbouring hex holes in a row
HEX_FLAT = 8.5     # hex hole across flats

# knurl notches (conical cuts)
N_NOTCH = 28
NOTCH_R = 3.73     # cone base radius at grid face
NOTCH_LEN = 12.1   # cone length
NOTCH_OFF = -0.5   # radial offset of cone axis from band surface (neg = inside)
NOTCH_PHASE = 0.4  # angular phase of the notch pattern (deg)
SEAM_ANG = 251.1

# inner slot groups
N_GROUP = 3
GROUP_ANG0 = 90.0  # angle of first group (local frame)
N_SLOT = 5
SLOT_W = 1.8
SLOT_LEN = 10.0
SLOT_PITCH = 3.3
SLOT_DEPTH = 0.8
SLOT_Z0 = L - 1.3   # axial position of slot nearest the rim

# orientation of the part axis in world space
AXIS_AZ = 34.71     # deg, azimuth of axis (from +X toward +Y)
AXIS_EL = 11.96     # deg, elevation of axis
ROLL = 0.0         # deg, roll about the axis

# ---------------- body of revolution ----------------
def arc_mid(c, r, a0, a1):
    am = math.radians((a0 + a1) / 2.0)
    return (c[0] + r * math.cos(am), c[1] + r * math.sin(am))


def arc_end(c, r, a):
    return (c[0] + r * math.cos(math.radians(a)), c[1] + r * math.sin(math.radians(a)))


z0 = LK                        # thread starts at the shoulder
gc = (RT + GW / 2.0, LK)       # centre of the relief groove in the shoulder face
sk = (
    cq.Workplane("XZ")
    .moveTo(0.0, 0.0)
    .lineTo(R1 - CH, 0.0)
    .lineTo(R1, CH)
    .lineTo(R1, LK - FK)
    .threePointArc(arc_mid((R1 - FK, LK - FK), FK, 0, 90), (R1 - FK, LK))
    .lineTo(RT + GW, LK)
    .threePointArc((gc[0], LK - GW / 2.0), (RT, LK))
    .lineTo(RT, z0 + 1.6 * TW)
    .lineTo(RT - TD, z0 + 2.1 * TW)
    .lineTo(RT, z0 + 2.6 * TW)
    .lineTo(RT, z0 + 4.0 * TW)
    .lineTo(RN, z0 + 4.5 * TW)
    .lineTo(RM, z0 + 5.0 * TW)
    .lineTo(RM, L - FR)
    .threePointArc(((RM + RI) / 2.0, L - FR + (RM - RI) / 2.0), (RI, L - FR))
    .lineTo(RI, TG)
    .lineTo(0.0, TG)
    .close()
)
body = sk.revolve(360, (0, 0, 0), (0, 1, 0))
# put the revolve seam on the lower side of the ring
body = body.rotate((0, 0, 0), (0, 0, 1), SEAM_ANG)

# ---------------- hex perforation ----------------
circ = HEX_PITCH / math.sqrt(3.0)  # cell circumradius (pointy-top rows along X)
row_h = HEX_PITCH * math.sqrt(3.0) / 2.0
pts = []
nr = int(RG / row_h) + 2
nc = int(RG / HEX_PITCH) + 2
for j in range(-nr, nr + 1):
    off = (HEX_PITCH / 2.0) if (j % 2) else 0.0
    for i in range(-nc - 1, nc + 1):
        x = i * HEX_PITCH + off
        y = j * row_h
        if math.hypot(x, y) < RG + HEX_PITCH * 0.5:
            pts.append((x, y))
hex_d = HEX_FLAT / math.cos(math.radians(30))  # circumscribed diameter of hole
# lattice points pre-rotated by -30 deg so that after rotating the whole pattern by +30 deg
# the rows run along local X and every hole has a vertex pointing along local Y
ca, sa = math.cos(math.radians(-30)), math.sin(math.radians(-30))
pts_r = [(x * ca - y * sa, x * sa + y * ca) for (x, y) in pts]
holes = (
    cq.Workplane("XY")
    .workplane(offset=-1.0)
    .pushPoints(pts_r)
    .polygon(6, hex_d)
    .extrude(TG + 2.0)
    .rotate((0, 0, 0), (0, 0, 1), 30)
)
zone = cq.Workplane("XY").workplane(offset=-1.0).circle(RG).extrude(TG + 2.0)
holes = holes.intersect(zone)
body = body.cut(holes)

# ---------------- conical notches on grip band ----------------
cones = []
zc = -0.5                      # start cones just outside the grid face
for k in range(N_NOTCH):
    a = NOTCH_PHASE + 360.0 * k / N_NOTCH
    h = NOTCH_LEN - zc
    cone = cq.Solid.makeCone(
        NOTCH_R * h / NOTCH_LEN, 0.0, h,
        cq.Vector(R1 + NOTCH_OFF, 0.0, zc),
        cq.Vector(0, 0, 1),
    )
    # built on +X so the cone seam faces radially outward, then swung into place
    cones.append(cone.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), a))
body = body.cut(cq.Workplane().add(cq.Compound.makeCompound(cones)))

# ---------------- inner slot groups ----------------
slots = None
for gi in range(N_GROUP):
    ga = GROUP_ANG0 + gi * 360.0 / N_GROUP
    for si in range(N_SLOT):
        z = SLOT_Z0 - si * SLOT_PITCH
        s = (
            cq.Workplane("YZ")
            .workplane(offset=RI - SLOT_DEPTH)
            .center(0, z)
            .slot2D(SLOT_LEN, SLOT_W, 0)
            .extrude(SLOT_DEPTH + 1.5)
            .rotate((0, 0, 0), (0, 0, 1), ga)
        )
        sv = s.val()
        slots = sv if slots is None else slots.fuse(sv)
body = body.cut(cq.Workplane().add(slots))

# ---------------- orient in world ----------------
part = body.val()
O = cq.Vector(0, 0, 0)
part = part.rotate(O, cq.Vector(0, 0, 1), ROLL + 90.0)
part = part.rotate(O, cq.Vector(0, 1, 0), 90.0 - AXIS_EL)
part = part.rotate(O, cq.Vector(0, 0, 1), AXIS_AZ)

result = cq.Workplane().add(part)
VIEW = {"azimuth": 45, "elevation": 26}
